import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0             # square body side
H = 24.8             # body height
R_CORNER = 6.0       # vertical corner radius
TOP_CH = 0.8         # chamfer on the top outer edge
BOT_CH = 0.4         # chamfer on the bottom outer edge

# central cavity (revolved profile): a 42 mm top opening (lip), then an
# undercut cone widening down to a large inner chamber, a thin floor with a
# 30 mm through bore
POCKET_R = 21.0      # radius of the top opening
POCKET_CH = 0.8      # chamfer at the top of the opening
LIP_DEPTH = 8.2      # depth of the lip (start of the undercut)
UNDERCUT_ANGLE = 32.0  # undercut cone angle from vertical
CHAMBER_R = 27.1     # radius of the inner chamber wall
FLOOR_T = 1.9        # floor thickness
BORE_R = 15.2        # through bore radius in the floor
BORE_CH = 0.3        # chamfer at the bottom of the through bore

BC_D = 38.8          # bolt circle of the 8 small holes in the floor
SMALL_D = 4.7
N_SMALL = 8

CB_OFF = 20.5        # top counterbore offset from centre (x and y)
CB_D = 12.6          # top blind counterbore
CB_DEPTH = 7.0
CT_OFF = 23.4        # bottom corner hole offset from centre (x and y)
CT_D = 6.8           # bottom blind hole in the corners
CT_DEPTH = 8.0

SIDE_D = 5.4         # radial hole in the -Y face
SIDE_CSK = 7.3       # countersink / boss diameter
SIDE_BOSS = 0.3      # low boss height around the radial hole
SIDE_DEPTH = 8.1     # axis depth below the top face

TXT_DZ = -0.2        # vertical shift of the text block
TXT_H = 0.2          # emboss height

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .rect(W, W)
    .extrude(H)
    .edges("|Z")
    .fillet(R_CORNER)
)
body = body.faces(">Z").edges().chamfer(TOP_CH)
body = body.faces("<Z").edges().chamfer(BOT_CH)

# ---------------- central cavity: one revolved profile ----------------
z_lip = H - LIP_DEPTH
z_chamber = z_lip - (CHAMBER_R - POCKET_R) / math.tan(math.radians(UNDERCUT_ANGLE))
z_floor = FLOOR_T
profile = [
    (0.0, -1.0),
    (BORE_R + BORE_CH + 1.0, -1.0),      # bottom chamfer cone, extended below the face
    (BORE_R, BORE_CH),
    (BORE_R, z_floor),                   # through bore
    (CHAMBER_R, z_floor),                # floor of the chamber
    (CHAMBER_R, z_chamber),              # chamber wall
    (POCKET_R, z_lip),                   # undercut cone up to the lip
    (POCKET_R, H - POCKET_CH),           # lip wall
    (POCKET_R + POCKET_CH + 1.0, H + 1.0),  # top chamfer cone, extended above the face
    (0.0, H + 1.0),
]
cavity = (
    cq.Workplane("XZ")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(cavity)

# 8 small through holes in the chamber floor
pts = [
    (BC_D / 2 * math.cos(2 * math.pi * i / N_SMALL), BC_D / 2 * math.sin(2 * math.pi * i / N_SMALL))
    for i in range(N_SMALL)
]
small = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(pts)
    .circle(SMALL_D / 2)
    .extrude(z_floor + 1.0 + 0.01)
)
body = body.cut(small)

# corner holes: blind counterbores from the top, blind holes from the bottom
cpts = [(sx * CB_OFF, sy * CB_OFF) for sx in (-1, 1) for sy in (-1, 1)]
cb = (
    cq.Workplane("XY")
    .workplane(offset=H - CB_DEPTH)
    .pushPoints(cpts)
    .circle(CB_D / 2)
    .extrude(CB_DEPTH + 1.0)
)
tpts = [(sx * CT_OFF, sy * CT_OFF) for sx in (-1, 1) for sy in (-1, 1)]
ct = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(tpts)
    .circle(CT_D / 2)
    .extrude(CT_DEPTH + 1.0)
)
body = body.cut(cb).cut(ct)

# radial hole through the -Y wall into the cavity, with low boss and countersink
z_side = H - SIDE_DEPTH
boss = cq.Solid.makeCylinder(
    SIDE_CSK / 2, SIDE_BOSS + 0.5, cq.Vector(0, -W / 2 + 0.5, z_side), cq.Vector(0, -1, 0)
)
body = body.union(cq.Workplane().add(boss))
side = cq.Solid.makeCylinder(
    SIDE_D / 2, W / 2 - POCKET_R + 3.0, cq.Vector(0, -W / 2 - 1.0, z_side), cq.Vector(0, 1, 0)
)
csk_r0 = SIDE_CSK / 2
csk_len = csk_r0 - SIDE_D / 2
y_face = -W / 2 - SIDE_BOSS
side_csk = cq.Solid.makeCone(
    csk_r0 + 0.5, SIDE_D / 2, csk_len + 0.5,
    cq.Vector(0, y_face - 0.5, z_side), cq.Vector(0, 1, 0)
)
body = body.cut(cq.Workplane().add(side)).cut(cq.Workplane().add(side_csk))


# ---------------- raised text "[ MTF ]" on +X, +Y and -X faces ----------------
SW = 1.1                      # stroke width
CAP_LO, CAP_HI = -2.47, 4.92  # letter z-range relative to mid-height
BR_LO, BR_HI = -3.5, 5.56     # bracket z-range relative to mid-height
F_MID = 0.78                  # lower edge of the middle bar of the F


def rect(x0, x1, z0, z1):
    return [(x0, z0), (x1, z0), (x1, z1), (x0, z1)]


def glyph_polys():
    lo, hi = CAP_LO + TXT_DZ, CAP_HI + TXT_DZ
    blo, bhi = BR_LO + TXT_DZ, BR_HI + TXT_DZ
    sh = SW * 0.9
    polys = []
    # brackets
    polys.append(rect(-22.0, -22.0 + SW, blo, bhi))
    polys.append(rect(-22.0 + SW - 0.01, -20.1, bhi - sh, bhi))
    polys.append(rect(-22.0 + SW - 0.01, -20.1, blo, blo + sh))
    polys.append(rect(21.8 - SW, 21.8, blo, bhi))
    polys.append(rect(20.0, 21.8 - SW + 0.01, bhi - sh, bhi))
    polys.append(rect(20.0, 21.8 - SW + 0.01, blo, blo + sh))
    # M: two stems + V
    mx0, mx1 = -14.7, -4.4
    mc = (mx0 + mx1) / 2
    polys.append(rect(mx0, mx0 + SW, lo, hi))
    polys.append(rect(mx1 - SW, mx1, lo, hi))
    polys.append([(mx0 + 0.2, hi), (mx0 + SW * 1.3, hi), (mc + SW * 0.6, lo + 0.3), (mc - SW * 0.6, lo + 0.3)])
    polys.append([(mx1 - SW * 1.3, hi), (mx1 - 0.2, hi), (mc + SW * 0.6, lo + 0.3), (mc - SW * 0.6, lo + 0.3)])
    # T
    polys.append(rect(-2.85, 6.1, hi - SW, hi))
    tc = (-2.85 + 6.1) / 2
    polys.append(rect(tc - SW / 2, tc + SW / 2, lo, hi - SW + 0.01))
    # F
    polys.append(rect(7.0, 7.0 + SW, lo, hi))
    polys.append(rect(7.0 + SW - 0.01, 14.7, hi - SW, hi))
    polys.append(rect(7.0 + SW - 0.01, 14.4, F_MID + TXT_DZ, F_MID + TXT_DZ + SW))
    return polys


def text_on(origin, xdir, normal):
    pl = cq.Plane(origin=origin, xDir=xdir, normal=normal)
    wp = cq.Workplane(pl).workplane(offset=-0.05)
    solid = None
    for poly in glyph_polys():
        s = wp.polyline(poly).close().extrude(TXT_H + 0.05)
        solid = s if solid is None else solid.union(s)
    return solid


z_mid = H / 2
for o, xd, n in [
    ((W / 2, 0, z_mid), (0, 1, 0), (1, 0, 0)),      # +X face, reads toward +Y
    ((0, W / 2, z_mid), (-1, 0, 0), (0, 1, 0)),     # +Y face, reads toward -X
    ((-W / 2, 0, z_mid), (0, -1, 0), (-1, 0, 0)),   # -X face, reads toward -Y
]:
    body = body.union(text_on(o, xd, n))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
